import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# drum (X axis is the drum / arm axis, part runs from x=0 to x=X_END)
COVER_R = 48.5        # end cover disk radius
COVER_T = 12.0        # end cover thickness (protrusion from drum face)
DRUM_R = 57.5         # drum radius
DRUM_X1 = 61.0        # end of drum
BAND_R = 60.0         # raised band radius
BAND_X1 = 77.0        # end of band
NECK_R = 43.0         # neck radius
NECK_FILLET = 14.0    # fillet band -> neck
DRUM_BOLTS = 15
DRUM_BOLT_PCD_R = 53.5

# lofted arm body
X_S1 = 95.0           # start of loft (round neck section)
X_S2 = 230.0          # second section (still roundish)
X_SM = 357.0          # third section (boxy, at king-pin axis)
X_S3 = 467.0          # set-back plane of the -Y part of the end face
X_END = 473.0         # end section / +Y part of the end face
SPLIT_Y = -41.0       # split between recessed and raised end-face parts
S2_HALF_W = 53.0
S2_RS = 53.0
S2_TOP = 41.0
S2_ZBR = -23.0        # lower crease height
S2_BOT = -41.5
S2_RC = 20.0
X_S25 = 300.0
S25_HALF_W = 67.5
S25_RS = 100.0
S25_TOP = 40.7
S25_ZBR = -27.5
S25_BOT = -40.2
S25_RC = 13.0
SM_HALF_W = 81.0
SM_RS = 250.0
SM_TOP = 40.2
SM_ZBR = -30.5
SM_BOT = -39.6
SM_RC = 8.0
S3_R = 106.0          # side arcs radius of end section
S3_TOP = 39.5
S3_BOT = -38.3
S3_RC = 7.0
CORNER_ANG = 21.5     # angular position of the lower crease on the round neck
S1_ANG_SIDE = 30.0    # vertex angles on the round neck matching the upper blends
S1_ANG_TOP = 50.0
TEAR_X = 308.0        # tear-drop boss on -Y flank
TEAR_Z = 4.0
TEAR_A = 36.0         # base half-length (x) of the tear-drop
TEAR_B = 13.0         # base half-height (z)
TEAR_H = 31.0         # loft length towards -Y

# vertical (king-pin) housing
VC_X = 361.0
VC_Y = 16.5
VC_R = 73.5
VC_ZBOT = -80.0
VC_ZTOP = 27.0
COVER2_R = 60.0
COVER2_ZBOT = -97.0
VC_BOLTS = 15
VC_BOLT_PCD_R = 67.0

# diamond pocket on top
POCKET_X = 359.0      # pocket centre
POCKET_Y = 11.0
POCKET_HDX = 72.0     # half diagonal along X at the top surface
POCKET_HDY = 67.0     # half diagonal along Y at the top surface
POCKET_RUN = 8.0      # horizontal run of the drafted pocket walls
POCKET_FLOOR = 31.0
POCKET_H = 9.0
POCKET_BOSS_R = 10.0
POCKET_BOSS_H = 4.0


# ---------------- helpers ----------------
def yz_pt(x, y, z):
    return cq.Vector(x, y, z)


def line(x, p0, p1):
    return cq.Edge.makeLine(yz_pt(x, *p0), yz_pt(x, *p1))


def arc_pts(x, pts):
    return cq.Edge.makeThreePointArc(*[yz_pt(x, *p) for p in pts])


def polar(r, deg):
    a = math.radians(deg)
    return (r * math.cos(a), r * math.sin(a))


def section_circle(x, r, ang_bot, ang_side, ang_top):
    """Round neck section split into 6 arcs matching the vertices of the other
    sections (lower creases at -ang_bot / 180+ang_bot)."""
    A = [-ang_bot, ang_side, ang_top, 180 - ang_top, 180 - ang_side, 180 + ang_bot]
    A.append(A[0] + 360)
    edges = []
    for i in range(6):
        a0, a1 = A[i], A[i + 1]
        edges.append(arc_pts(x, [polar(r, a0), polar(r, 0.5 * (a0 + a1)), polar(r, a1)]))
    return cq.Wire.assembleEdges(edges)


def rounded_section(x, hw, Rs, top, z_br, bot_mid, rc):
    """Section with side arcs (radius Rs, centre on z=0 at y=+-(hw-Rs)), a flat top
    at z=top joined to the sides by fillets of radius rc, and a bottom edge from
    BL to BR (BR on the side arc at z=z_br); bot_mid=None gives a straight bottom,
    otherwise the bottom is an arc through (0, bot_mid).
    Returns a 6-edge wire starting at BR going up the right side."""
    c0 = hw - Rs                                   # side arc centre (y)
    zc = top - rc
    yc = c0 + math.sqrt((Rs - rc) ** 2 - zc ** 2)   # fillet centre
    k = Rs / (Rs - rc)
    ps = (c0 + (yc - c0) * k, zc * k)               # tangent point on side arc
    pt = (yc, top)                                  # tangent point on top line
    br = (c0 + math.sqrt(Rs ** 2 - z_br ** 2), z_br)
    bl = (-br[0], br[1])
    a_br = math.atan2(br[1], br[0] - c0)
    a_ps = math.atan2(ps[1], ps[0] - c0)
    am = 0.5 * (a_br + a_ps)
    side_mid = (c0 + Rs * math.cos(am), Rs * math.sin(am))
    a_f = 0.5 * (math.atan2(ps[1] - zc, ps[0] - yc) + math.pi / 2)
    cm = (yc + rc * math.cos(a_f), zc + rc * math.sin(a_f))
    m = lambda p: (-p[0], p[1])
    edges = [
        arc_pts(x, [br, side_mid, ps]),
        arc_pts(x, [ps, cm, pt]),
        line(x, pt, m(pt)),
        arc_pts(x, [m(pt), m(cm), m(ps)]),
        arc_pts(x, [m(ps), m(side_mid), bl]),
    ]
    if bot_mid is None:
        edges.append(line(x, bl, br))
    else:
        edges.append(arc_pts(x, [bl, (0.0, bot_mid), br]))
    return cq.Wire.assembleEdges(edges)


# ---------------- drum + neck (revolved) ----------------
c = NECK_FILLET
drum_prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(0, COVER_R - 2.0)
    .lineTo(2.0, COVER_R)
    .lineTo(COVER_T, COVER_R)
    .lineTo(COVER_T, DRUM_R - 1.5)
    .lineTo(COVER_T + 1.5, DRUM_R)
    .lineTo(DRUM_X1, DRUM_R)
    .lineTo(DRUM_X1, BAND_R)
    .lineTo(BAND_X1, BAND_R)
    .lineTo(BAND_X1, NECK_R + c)
    .threePointArc(
        (BAND_X1 + c - c / math.sqrt(2), NECK_R + c - c / math.sqrt(2)),
        (BAND_X1 + c, NECK_R),
    )
    .lineTo(X_S1, NECK_R)
    .lineTo(X_S1, 0)
    .close()
)
drum = drum_prof.revolve(360, (0, 0, 0), (1, 0, 0))

# drum end bolts (socket heads on the drum end face)
bolts = None
for i in range(DRUM_BOLTS):
    a = 2 * math.pi * i / DRUM_BOLTS
    y = DRUM_BOLT_PCD_R * math.cos(a)
    z = DRUM_BOLT_PCD_R * math.sin(a)
    b = (
        cq.Workplane("YZ", origin=(COVER_T - 4.0, y, z))
        .circle(2.8)
        .extrude(4.5)
    )
    bolts = b if bolts is None else bolts.union(b)
drum = drum.union(bolts)

# ---------------- lofted arm ----------------
w1 = section_circle(X_S1, NECK_R, CORNER_ANG, S1_ANG_SIDE, S1_ANG_TOP)
w2 = rounded_section(X_S2, S2_HALF_W, S2_RS, S2_TOP, S2_ZBR, S2_BOT, S2_RC)
w25 = rounded_section(X_S25, S25_HALF_W, S25_RS, S25_TOP, S25_ZBR, S25_BOT, S25_RC)
wm = rounded_section(X_SM, SM_HALF_W, SM_RS, SM_TOP, SM_ZBR, SM_BOT, SM_RC)
w3 = rounded_section(X_END, S3_R, S3_R, S3_TOP, S3_BOT, None, S3_RC)
arm = cq.Workplane("XY").add(cq.Solid.makeLoft([w1, w2, w25, wm, w3], False))

# the -Y part of the end face is set back (X_END - X_S3)
setback = (
    cq.Workplane("XY")
    .box(30.0, 200.0, 200.0, centered=(False, False, True))
    .translate((X_S3, SPLIT_Y - 200.0, 0.0))
)
arm = arm.cut(setback)

body = drum.union(arm)

# ---------------- vertical king-pin housing ----------------
vc = (
    cq.Workplane("XY", origin=(VC_X, VC_Y, VC_ZBOT))
    .transformed(rotate=(0, 0, 180))
    .circle(VC_R)
    .extrude(VC_ZTOP - VC_ZBOT)
)
cover2 = (
    cq.Workplane("XY", origin=(VC_X, VC_Y, COVER2_ZBOT))
    .transformed(rotate=(0, 0, 180))
    .circle(COVER2_R)
    .extrude(VC_ZBOT - COVER2_ZBOT + 1.0)
    .faces("<Z").edges()
    .chamfer(1.5)
)
body = body.union(vc).union(cover2)
for i in range(VC_BOLTS):
    a = 2 * math.pi * (i + 0.5) / VC_BOLTS
    b = (
        cq.Workplane("XY", origin=(VC_X + VC_BOLT_PCD_R * math.cos(a),
                                   VC_Y + VC_BOLT_PCD_R * math.sin(a), VC_ZBOT - 6.5))
        .polygon(6, 8.0)
        .extrude(6.6)
    )
    body = body.union(b)

# ---------------- diamond pocket on top ----------------
# rhombus (diagonals along X and Y) with drafted walls and a small central boss
run = POCKET_RUN                              # horizontal run of the drafted walls
hyp = math.hypot(POCKET_HDX, POCKET_HDY)
ax = POCKET_HDX - run * hyp / POCKET_HDY      # floor half diagonals
ay = POCKET_HDY - run * hyp / POCKET_HDX
ext = 2.0                                     # extend the frustum above the top surface
kx = (POCKET_HDX - ax) / POCKET_H
ky = (POCKET_HDY - ay) / POCKET_H
bx = POCKET_HDX + kx * ext
by = POCKET_HDY + ky * ext
pocket = (
    cq.Workplane("XY", origin=(POCKET_X, POCKET_Y, POCKET_FLOOR))
    .polyline([(ax, 0), (0, ay), (-ax, 0), (0, -ay)])
    .close()
    .workplane(offset=POCKET_H + ext)
    .polyline([(bx, 0), (0, by), (-bx, 0), (0, -by)])
    .close()
    .loft(ruled=True)
)
pocket = pocket.union(
    cq.Workplane("XY", origin=(POCKET_X, POCKET_Y, POCKET_FLOOR + POCKET_H + ext))
    .polyline([(bx, 0), (0, by), (-bx, 0), (0, -by)])
    .close()
    .extrude(20.0)
)
body = body.cut(pocket)
pboss = (
    cq.Workplane("XY", origin=(POCKET_X, VC_Y, POCKET_FLOOR - 0.5))
    .circle(POCKET_BOSS_R)
    .extrude(POCKET_BOSS_H + 0.5)
)
body = body.union(pboss)

# ---------------- end face bosses / knob ----------------
END_BOSS_R = 8.4
for yb in (-7.0, 75.0):
    eb = cq.Workplane("YZ", origin=(X_END - 1.0, yb, 0.0)).circle(END_BOSS_R).extrude(3.0)
    body = body.union(eb)
knob = cq.Workplane("YZ", origin=(X_S3 - 1.0, -74.0, 0.0)).circle(8.0).extrude(10.0)
body = body.union(knob)

# ---------------- bosses on the +Y flank ----------------
# round boss near the end of the +Y flank
sb1 = cq.Workplane("XZ", origin=(447.0, 106.0, 3.0)).circle(9.0).extrude(20.0)
# king-pin housing side boss (axis Y)
sb2 = cq.Workplane("XZ", origin=(333.0, 105.6, 0.0)).circle(10.5).extrude(40.0)
body = body.union(sb1).union(sb2)
# tapped holes in the two flank bosses
h1 = cq.Workplane("XZ", origin=(447.0, 106.5, 3.0)).circle(3.5).extrude(8.0)
h2 = cq.Workplane("XZ", origin=(333.0, 106.0, 0.0)).circle(4.5).extrude(12.0)
body = body.cut(h1).cut(h2)
# small cast pads on the +Y flank
pad1 = cq.Workplane("XZ", origin=(281.0, 73.0, 2.5)).slot2D(30.0, 8.0, 90).extrude(16.0)
pad2 = cq.Workplane("XZ", origin=(178.0, 50.0, 9.0)).rect(12.0, 12.0).extrude(10.0).edges("|Y").fillet(3.0)
pad3 = cq.Workplane("XZ", origin=(140.0, 47.0, 1.0)).slot2D(16.0, 7.0, 0).extrude(10.0)
body = body.union(pad1).union(pad2).union(pad3)

# ---------------- tear-drop boss on the -Y flank ----------------
tear = (
    cq.Workplane("XZ", origin=(TEAR_X, -56.0, TEAR_Z))
    .ellipse(TEAR_A, TEAR_B)
    .workplane(offset=TEAR_H)
    .ellipse(3.0, 1.5)
    .loft()
)
body = body.union(tear)

# ---------------- clevis lug on the king-pin housing ----------------
CLV_X0, CLV_X1 = 257.0, 300.0
CLV_Y0, CLV_Y1 = 24.0, 56.0
CLV_Z0, CLV_Z1 = -96.0, -74.0
clevis = (
    cq.Workplane("XY")
    .box(CLV_X1 - CLV_X0, CLV_Y1 - CLV_Y0, CLV_Z1 - CLV_Z0, centered=False)
    .translate((CLV_X0, CLV_Y0, CLV_Z0))
    .edges("|Y and <X")
    .fillet(5.0)
)
slot = (
    cq.Workplane("XY")
    .box(32.0, 11.0, 30.0, centered=False)
    .translate((CLV_X0 - 2.0, 0.5 * (CLV_Y0 + CLV_Y1) - 5.5, CLV_Z0 - 2.0))
)
pin_hole = cq.Workplane("XZ", origin=(266.0, CLV_Y1 + 1.0, -86.0)).circle(6.5).extrude(CLV_Y1 - CLV_Y0 + 2.0)
clevis = clevis.cut(slot).cut(pin_hole)
body = body.union(clevis)

result = body
